import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PL_L = 76.0        # wall plate length (Y)
PL_T = 8.6         # wall plate thickness (X)
H = 30.8           # overall height (Z) of plate and arm
PL_R = 3.8         # rounded front corners of the plate

ARM_Y0 = 24.4      # arm lower (-Y) face
ARM_Y1 = 45.6      # arm upper (+Y) edge line (top/bottom faces end here)
ARM_BULGE = 5.7    # convex bulge of the arm's +Y face at mid height
X_END = 92.6       # outer end of the hook (X)
LIP_T = 6.6        # thickness of the hook lip (X)
LIP_Y1 = 57.2      # lip tip edge line (Y)
LIP_BULGE = 4.3    # convex bulge of the lip tip at mid height
LIP_R = 1.5        # rounding of lip tip corners
BEND_R = 14.6      # outer bend radius of hook
ROOT_R = 7.0       # fillet between plate and arm (-Y side)

HOLE_D = 7.4       # screw clearance hole
CB_D = 12.7        # counterbore diameter
CB_DEPTH = 3.5     # counterbore depth
HOLE_OFF = 9.84    # hole centre distance from plate ends

RIB_H = 2.4        # rear locating rib height (-X)
RIB_BASE = 6.0     # rib width at base (Z)
RIB_TOP = 3.8      # rib width at top (Z)
RIB_GAP = 7.8      # rib interruption at each hole (at rib root)
RIB_CH = 1.2       # slope of the rib ends in plan view

POCK_X = (28.2, 66.3)   # centres of the two cross pockets on the arm's +Y face
POCK_W = 8.6            # vertical slot width (X)
POCK_W_END = 10.4       # slot width near the top / bottom faces (X)
POCK_STEP = 8.9         # depth (Z) of the wider part from top / bottom faces
POCK_FLOOR = 47.3       # vertical slot floor (Y)
POCK_HL = 18.8          # horizontal slot length (X)
POCK_HH = 8.6           # horizontal slot height (Z)
POCK_HFLOOR = 44.6      # horizontal slot floor (Y)

ZC = H / 2.0
ARM_TOP = ARM_Y1 + ARM_BULGE
LIP_TOP = LIP_Y1 + LIP_BULGE
X_LIP = X_END - LIP_T

# ---------------- main body: T profile extruded in Z ----------------
pts = [
    (0.0, 0.0),
    (PL_T, 0.0),
    (PL_T, ARM_Y0),
    (X_END, ARM_Y0),
    (X_END, LIP_TOP),
    (X_LIP, LIP_TOP),
    (X_LIP, ARM_TOP),
    (PL_T, ARM_TOP),
    (PL_T, PL_L),
    (0.0, PL_L),
]
body = cq.Workplane("XY").polyline(pts).close().extrude(H)


def fillet_vertical(wp, x, y, r):
    return wp.edges("|Z").edges(
        cq.selectors.NearestToPointSelector((x, y, ZC))
    ).fillet(r)


body = fillet_vertical(body, PL_T, 0.0, PL_R)
body = fillet_vertical(body, PL_T, PL_L, PL_R)
body = fillet_vertical(body, PL_T, ARM_Y0, ROOT_R)
body = fillet_vertical(body, X_END, ARM_Y0, BEND_R)


def bulge_cutter(x0, x1, y_edge, sag, y_lo, y_hi):
    """Region above a circular arc (axis along X) -> leaves a convex face."""
    r = ((H / 2.0) ** 2 + sag ** 2) / (2.0 * sag)
    yc = y_edge + sag - r
    box = (
        cq.Workplane("XY")
        .box(x1 - x0, y_hi - y_lo, H + 4.0, centered=False)
        .translate((x0, y_lo, -2.0))
    )
    cyl = cq.Workplane("YZ").workplane(offset=x0 - 1.0).center(yc, ZC).circle(r).extrude(
        x1 - x0 + 2.0
    )
    return box.cut(cyl)


# convex +Y face of the arm
body = body.cut(bulge_cutter(PL_T, X_LIP, ARM_Y1, ARM_BULGE, ARM_Y1 - 2.0, ARM_TOP + 2.0))
# convex tip of the hook lip, edges softened
body = body.cut(bulge_cutter(X_LIP - 1.0, X_END + 1.0, LIP_Y1, LIP_BULGE, LIP_Y1 - 2.0, LIP_TOP + 2.0))
body = body.edges(cq.selectors.NearestToPointSelector((X_END, LIP_TOP, ZC))).fillet(LIP_R)
body = body.edges(cq.selectors.NearestToPointSelector((X_LIP, LIP_TOP, ZC))).fillet(LIP_R)

# ---------------- cross shaped pockets in the arm's +Y face ----------------
# a vertical slot through the bulge (stepped wider near the top and bottom
# faces) crossed at mid height by a deeper horizontal slot
def ybox(x0, x1, y0, z0, z1):
    y1 = ARM_TOP + 5.0
    return (
        cq.Workplane("XY")
        .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
        .translate((x0, y0, z0))
    )


for xc in POCK_X:
    hw_n = POCK_W / 2.0
    hw_w = POCK_W_END / 2.0
    cut = ybox(xc - hw_n, xc + hw_n, POCK_FLOOR, -2.0, H + 2.0)
    cut = cut.union(ybox(xc - hw_w, xc + hw_w, POCK_FLOOR, H - POCK_STEP, H + 2.0))
    cut = cut.union(ybox(xc - hw_w, xc + hw_w, POCK_FLOOR, -2.0, POCK_STEP))
    cut = cut.union(
        ybox(xc - POCK_HL / 2.0, xc + POCK_HL / 2.0, POCK_HFLOOR, ZC - POCK_HH / 2.0, ZC + POCK_HH / 2.0)
    )
    body = body.cut(cut)

# ---------------- rear locating rib (interrupted at the holes) ----------------
hole_ys = (HOLE_OFF, PL_L - HOLE_OFF)
segs = [
    (0.0, hole_ys[0] - RIB_GAP / 2.0),
    (hole_ys[0] + RIB_GAP / 2.0, hole_ys[1] - RIB_GAP / 2.0),
    (hole_ys[1] + RIB_GAP / 2.0, PL_L),
]
rib_prof = [
    (0.0, ZC - RIB_BASE / 2.0),
    (-RIB_H, ZC - RIB_TOP / 2.0),
    (-RIB_H, ZC + RIB_TOP / 2.0),
    (0.0, ZC + RIB_BASE / 2.0),
]
for y0, y1 in segs:
    # trapezoidal section along Y ...
    rib = (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .polyline(rib_prof)
        .close()
        .extrude(-(y1 - y0))
    )
    # ... with sloped (chamfered) ends in plan view
    c0 = RIB_CH
    c1 = RIB_CH
    plan = (
        cq.Workplane("XY")
        .polyline([(0.1, y0), (-RIB_H, y0 + c0), (-RIB_H, y1 - c1), (0.1, y1)])
        .close()
        .extrude(H)
    )
    body = body.union(rib.intersect(plan))

# ---------------- counterbored screw holes through the plate ----------------
# (cutting cylinders are spun about their axis so the face seams sit on the
#  hidden side of the bores)
for hy in hole_ys:
    axis_p0 = (0.0, hy, ZC)
    axis_p1 = (1.0, hy, ZC)
    thru = (
        cq.Workplane("YZ")
        .workplane(offset=-RIB_H - 2.0)
        .center(hy, ZC)
        .circle(HOLE_D / 2.0)
        .extrude(PL_T + RIB_H + 4.0)
        .rotate(axis_p0, axis_p1, 120)
    )
    cb = (
        cq.Workplane("YZ")
        .workplane(offset=PL_T - CB_DEPTH)
        .center(hy, ZC)
        .circle(CB_D / 2.0)
        .extrude(CB_DEPTH + 2.0)
        .rotate(axis_p0, axis_p1, 135)
    )
    body = body.cut(thru).cut(cb)

result = body
